import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0        # length along Y
H = 80.0         # height along Z
T = 15.0         # depth along X (closed face at +X, open side at -X)
t = 1.2          # wall thickness
r_out = 1.1      # outer edge rounding

# groove along the top edge on the open side
g_r = 5.6        # groove radius
g_c = 6.8        # groove centre below top
g_wall = 1.2     # wall around groove
lip_r = 0.8      # rounding of the lip nose

# notch in the -Y end wall (open side)
n_z0 = 35.0      # from top
n_h = 10.0
n_d = 2.6

# snap hooks on +Y end
hk_z = [40.8, 50.8]   # centre depth below top
hk_h = 4.5
hk_p = 2.8            # protrusion beyond +Y face
hk_x = 3.2            # extent along X from open face
hk_rz = 0.8           # rounding of the hook tip seen from above
hk_rx = 1.0           # chamfer of the hook tip top / bottom

# corner screw bosses
b_r = 2.2
b_off = 1.4      # boss axis offset from the inner wall faces
b_hole = 0.75

# inner rib near +Y end
rib_gap = 29.5   # from +Y inner wall face to rib face
rib_t = 1.2
rib_y = L / 2 - t - rib_gap - rib_t / 2
rib_top = 29.0   # from top

VIEW = {"azimuth": 45, "elevation": 26}

x0 = -T / 2      # open face
x1 = T / 2       # closed face

# ---------------- outer body ----------------
gz = H - g_c                     # groove axis height
body = cq.Workplane("XY").box(T, L, H).translate((0, 0, H / 2))
# round every outer edge except the rim of the open side
open_rim = cq.selectors.BoxSelector((x0 - 0.1, -L, -1), (x0 + 0.1, L, H + 1))
body = body.edges(cq.selectors.InverseSelector(open_rim)).fillet(r_out)
# groove along the top of the open side
groove = cq.Workplane("XZ").center(x0, gz).circle(g_r).extrude(L, both=True)
body = body.cut(groove)
# round the nose of the lip above the groove
nose = (cq.Workplane("XY").box(lip_r + 1.0, L + 2, lip_r + 1.0)
        .translate((x0 + (lip_r - 1.0) / 2, 0, H + (1.0 - lip_r) / 2)))
nose_keep = (cq.Workplane("XZ").center(x0 + lip_r, H - lip_r)
             .circle(lip_r).extrude(L + 2, both=True))
nose = nose.cut(nose_keep)
body = body.cut(nose)

# cavity (leaves a tube of wall around the groove)
clip = cq.Workplane("XY").box(T, L, H).translate((0, 0, H / 2))
house = (cq.Workplane("XZ").center(x0, gz).circle(g_r + g_wall)
         .extrude(L / 2, both=True))
cav = (cq.Workplane("XY")
       .box(T - t + 1.0, L - 2 * t, H - 2 * t)
       .translate(((x0 - 1.0 + x1 - t) / 2, 0, H / 2)))
cav = cav.cut(house)
body = body.cut(cav)

# corner bosses
by = L / 2 - t - b_off
zb_lo = t + b_off
zb_hi = gz - g_r - g_wall - b_off
for yy in (-by, by):
    for zz in (zb_lo, zb_hi):
        boss = (cq.Workplane("YZ").workplane(offset=x0)
                .center(yy, zz).circle(b_r).extrude(T - t))
        boss = boss.intersect(clip)
        body = body.union(boss)
        hole = (cq.Workplane("YZ").workplane(offset=x0 - 1)
                .center(yy, zz)
                .circle(b_hole).extrude(T - t - 1))
        body = body.cut(hole)

# inner rib
rib = (cq.Workplane("XY")
       .box(T - t, rib_t, H - rib_top - t)
       .translate((x0 + (T - t) / 2, rib_y, t + (H - rib_top - t) / 2)))
body = body.union(rib)

# notch in -Y end wall
notch = (cq.Workplane("XY").box(2 * n_d, 3 * t, n_h)
         .translate((x0, -L / 2, H - n_z0 - n_h / 2)))
body = body.cut(notch)

# snap hooks on +Y end
for hz in hk_z:
    hook = (cq.Workplane("XY").box(hk_x, hk_p + t, hk_h)
            .translate((x0 + hk_x / 2, L / 2 - t + (hk_p + t) / 2, H - hz)))
    hook = hook.edges("|X and >Y").chamfer(hk_rx)
    hook = hook.faces(">Y").edges("|Z and >X").fillet(hk_rz)
    body = body.union(hook)

result = body
